import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
MODULE = 2.5            # gear module
TEETH = 16              # number of teeth
PRESSURE_ANGLE = 20.0   # degrees
ADDENDUM = 1.0          # x module
DEDENDUM = 1.25         # x module
FACE_WIDTH = 12.85      # gear thickness (along Z)
BORE_D = 6.5            # centre bore diameter
BORE_SEAM_ANG = 45.0     # angular position of the bore's cylinder seam (deg)
INV_PTS = 8             # sample points per involute flank (spline)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived geometry ----------------
rp = MODULE * TEETH / 2.0                 # pitch radius
ra = rp + ADDENDUM * MODULE               # tip radius
rf = rp - DEDENDUM * MODULE               # root radius
alpha = math.radians(PRESSURE_ANGLE)
rb = rp * math.cos(alpha)                 # base radius


def inv(a):
    return math.tan(a) - a


# half angular tooth thickness at the base circle
psi_b = math.pi / (2 * TEETH) + inv(alpha)
pitch_ang = 2 * math.pi / TEETH


def half_thick(r):
    """half angular tooth thickness at radius r (r >= rb)"""
    a = math.acos(rb / r)
    return psi_b - inv(a)


def polar(r, th):
    return (r * math.cos(th), r * math.sin(th))


def flank_points(center, side):
    """involute flank points from base circle (or root) to tip.
    side = +1 -> flank on the CCW side of the tooth, -1 -> CW side."""
    r0 = max(rb, rf)
    pts = []
    for i in range(INV_PTS):
        r = r0 + (ra - r0) * i / (INV_PTS - 1)
        pts.append(polar(r, center + side * half_thick(r)))
    return pts


# ---------------- build the gear outline as one closed wire ----------------
def flank_edge(c, side):
    """one smooth flank face: radial run-out from the root circle blended
    into the involute up to the tip circle (single spline, root -> tip)."""
    pts = []
    if rf < rb:
        pts.append(polar(rf, c + side * psi_b))
    pts += flank_points(c, side)
    vecs = [cq.Vector(x, y, 0) for x, y in pts]
    beta = c + side * psi_b                       # involute start angle
    t_tip = math.tan(math.acos(rb / ra))          # involute roll parameter at tip
    t0 = cq.Vector(math.cos(beta), math.sin(beta), 0)          # radial at root
    t1 = cq.Vector(math.cos(beta - side * t_tip),
                   math.sin(beta - side * t_tip), 0)           # involute tangent at tip
    return vecs, t0, t1


edges = []
for k in range(TEETH):
    c = k * pitch_ang                      # tooth centre angle (tooth on +X)
    cw, t0_cw, t1_cw = flank_edge(c, -1)      # root -> tip
    ccw, t0_ccw, t1_ccw = flank_edge(c, +1)   # root -> tip
    # CW flank going outward
    edges.append(cq.Edge.makeSpline(cw, tangents=[t0_cw, t1_cw]))
    # tip arc
    tip_mid = cq.Vector(*polar(ra, c), 0)
    edges.append(cq.Edge.makeThreePointArc(cw[-1], tip_mid, ccw[-1]))
    # CCW flank going inward (build outward then reverse the point order)
    rev = list(reversed(ccw))
    edges.append(cq.Edge.makeSpline(rev, tangents=[-t1_ccw, -t0_ccw]))
    # root arc to the next tooth
    root_end = rev[-1]
    nxt = cq.Vector(*polar(rf, c + pitch_ang - psi_b), 0)
    mid = cq.Vector(*polar(rf, c + pitch_ang / 2.0), 0)
    edges.append(cq.Edge.makeThreePointArc(root_end, mid, nxt))

outline = cq.Wire.assembleEdges(edges)
face = cq.Face.makeFromWires(outline)
gear = cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, FACE_WIDTH)))

# centre bore (through), cylinder seam placed at BORE_SEAM_ANG
bore = cq.Solid.makeCylinder(BORE_D / 2.0, FACE_WIDTH + 2.0,
                             cq.Vector(0, 0, -1.0), cq.Vector(0, 0, 1))
bore = bore.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), BORE_SEAM_ANG)
gear = gear.cut(cq.Workplane("XY").add(bore))

result = gear
